import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FRAME_L = 400.0      # frame length along X
FRAME_W = 250.0      # frame depth along Y
FRAME_H = 50.0       # frame height along Z
WALL = 10.0          # frame wall thickness

PIN_X = 150.0        # leg pivot offset from frame centre (along X)
CRANK_R = 50.0       # crank length (centre shaft -> crank pin)
CRANK_DEG = 166.6    # front crank angle (deg, from +X toward +Z)
LEG_L = 375.0        # leg length, top pivot -> foot hole
LEG_MID = 250.0      # leg: top pivot -> connecting-link pivot
LINK_L = 300.0       # connecting link length (crank pin -> leg pivot)

BAR_W = 25.0         # width of every flat bar (legs, links, crank)
BAR_T = 10.0         # thickness of every flat bar
HOLE_D = 15.0        # pivot hole diameter
ROD_D = 15.0         # cross shaft diameter
SPACER_D = 18.0      # spacer ring outer diameter (link 'C' to leg joint)

HALF_W = FRAME_W / 2.0


# ---------------- helpers ----------------
def circle_intersect_lower(c0, r0, c1, r1):
    """Lower (min z) intersection of two circles in the XZ plane."""
    dx, dz = c1[0] - c0[0], c1[1] - c0[1]
    d = math.hypot(dx, dz)
    a = (r0 * r0 - r1 * r1 + d * d) / (2.0 * d)
    h = math.sqrt(max(r0 * r0 - a * a, 0.0))
    ex, ez = dx / d, dz / d
    bx, bz = c0[0] + a * ex, c0[1] + a * ez
    p1 = (bx - h * ez, bz + h * ex)
    p2 = (bx + h * ez, bz - h * ex)
    return p1 if p1[1] < p2[1] else p2


def flat_bar(p_a, p_b, y_outer, y_inner, holes):
    """Flat bar with full-round ends centred on p_a and p_b (x, z points in
    the XZ plane), spanning Y between y_inner and y_outer.
    holes: pivot hole positions as fractions of the distance a -> b."""
    dx, dz = p_b[0] - p_a[0], p_b[1] - p_a[1]
    L = math.hypot(dx, dz)
    ux, uz = dx / L, dz / L
    mx, mz = (p_a[0] + p_b[0]) / 2.0, (p_a[1] + p_b[1]) / 2.0
    y_hi = max(y_outer, y_inner)
    t = abs(y_outer - y_inner)
    plane = cq.Plane(origin=(mx, y_hi, mz), xDir=(ux, 0, uz), normal=(0, -1, 0))
    bar = cq.Workplane(plane).slot2D(L + BAR_W, BAR_W, 0).extrude(t)
    if holes:
        pts = [((f - 0.5) * L, 0.0) for f in holes]
        cutters = (
            cq.Workplane(plane)
            .pushPoints(pts)
            .circle(HOLE_D / 2.0)
            .extrude(t)
        )
        bar = bar.cut(cutters)
    return bar


# ---------------- frame (open rectangular box) ----------------
frame = (
    cq.Workplane("XY")
    .box(FRAME_L, FRAME_W, FRAME_H)
    .cut(cq.Workplane("XY").box(FRAME_L - 2 * WALL, FRAME_W - 2 * WALL, FRAME_H + 2))
)
# pivot holes through the long walls (legs) and the shaft bore
hole_cut = (
    cq.Workplane("XZ", origin=(0, HALF_W + 1, 0))
    .pushPoints([(-PIN_X, 0), (PIN_X, 0)])
    .circle(HOLE_D / 2.0)
    .extrude(FRAME_W + 2)
)
rod_bore = (
    cq.Workplane("XZ", origin=(0, HALF_W + 1, 0))
    .circle(ROD_D / 2.0)
    .extrude(FRAME_W + 2)
)
frame = frame.cut(hole_cut).cut(rod_bore)

# ---------------- cross shaft ----------------
rod = (
    cq.Workplane("XZ", origin=(0, HALF_W, 0))
    .circle(ROD_D / 2.0)
    .extrude(FRAME_W)
    .rotate((0, 0, 0), (0, 1, 0), 130)  # park the cylinder seam underneath
)

parts = [frame, rod]


# ---------------- one side of the leg mechanism ----------------
def side(sign, crank_deg):
    """Leg mechanism on one long side of the frame.
    sign=-1 : front side (-Y), sign=+1 : back side (+Y).
    Layer 1 (against the frame wall): both legs and the crank.
    Layer 2: link 'B' from the crank pin to one leg.
    Layer 3: link 'C' from the crank pin to the other leg (with a spacer
    ring filling layer 2 at that joint).
    The back side is the front arrangement turned half a turn about Z,
    driven by the opposite arm of the same crank shaft."""
    # Y extents (outer, inner) of bar layer n counted outward from the wall
    def layer(n):
        y_in = sign * (HALF_W + (n - 1) * BAR_T)
        y_out = sign * (HALF_W + n * BAR_T)
        return y_out, y_in

    th = math.radians(crank_deg)
    o = (0.0, 0.0)
    p2 = (CRANK_R * math.cos(th), CRANK_R * math.sin(th))

    # leg pivots: 'B' leg and 'C' leg
    xb = -PIN_X if sign < 0 else PIN_X
    xc = -xb
    out = []
    for xp, lay in ((xb, 2), (xc, 3)):
        top = (xp, 0.0)
        m = circle_intersect_lower(top, LEG_MID, p2, LINK_L)
        ux, uz = (m[0] - top[0]) / LEG_MID, (m[1] - top[1]) / LEG_MID
        foot = (top[0] + ux * LEG_L, top[1] + uz * LEG_L)
        # leg in layer 1 with holes at top, link pivot and foot
        out.append(
            flat_bar(top, foot, *layer(1), holes=[0.0, LEG_MID / LEG_L, 1.0])
        )
        # connecting link from crank pin to leg pivot
        out.append(flat_bar(p2, m, *layer(lay), holes=[0.0, 1.0]))
        if lay == 3:
            # spacer ring filling the empty layer 2 at the leg joint
            y_out, y_in = layer(2)
            ring = (
                cq.Workplane("XZ", origin=(0, max(y_out, y_in), 0))
                .circle(SPACER_D / 2.0)
                .circle(HOLE_D / 2.0)
                .extrude(BAR_T)
                .rotate((0, 0, 0), (0, 1, 0), 130)  # seam to the far side
                .translate((m[0], 0, m[1]))
            )
            out.append(ring)
    # crank in layer 1 (solid at the shaft end)
    out.append(flat_bar(o, p2, *layer(1), holes=[1.0]))
    return out


parts += side(-1, CRANK_DEG)
parts += side(+1, CRANK_DEG - 180.0)

result = cq.Workplane("XY").newObject(
    [cq.Compound.makeCompound([p.val() for p in parts])]
)

VIEW = {"azimuth": 45, "elevation": 26}
